import math
import cadquery as cq

# Countersunk (flat) head machine screw, head at the bottom, thread pointing up (+Z).
# The thread is a real right-hand helical 60 deg V thread with a rounded root and a
# small crest flat; the end of the screw is a flat cut through the thread.

# ---------------- driving dimensions (mm) ----------------
D_MAJOR = 5.0          # thread major diameter
D_MINOR = 3.80         # thread minor (root) diameter
PITCH = 1.037          # thread pitch (right hand)
FLANK_ANGLE = 60.0     # included thread angle (deg)
CREST_FLAT = PITCH / 8.0
HEAD_D = 9.54          # countersunk head diameter
HEAD_MARGIN = 1.16     # cylindrical edge height of the head
CSK_ANGLE = 92.0       # included countersink angle (deg)
CONE_TOP_D = 4.96      # diameter where the countersink meets the shank (just under D_MAJOR)
SHANK_LEN = 14.75      # length from top of the cone to the end of the screw
THREAD_PHASE = 0.48    # a crest on +X lies this many pitches below the end face
SEAM_ANGLE = 45.0      # where the revolve seam of the head sits (cosmetic only)

# ---------------- derived ----------------
R_MAJ = D_MAJOR / 2.0
R_MIN = D_MINOR / 2.0
R_HEAD = HEAD_D / 2.0
CONE_TOP_R = CONE_TOP_D / 2.0
CONE_H = (R_HEAD - CONE_TOP_R) / math.tan(math.radians(CSK_ANGLE / 2.0))
Z_CONE_TOP = HEAD_MARGIN + CONE_H
Z_TOP = Z_CONE_TOP + SHANK_LEN

# ---------------- countersunk head (revolved profile) ----------------
head = (
    cq.Workplane("XZ")
    .polyline([
        (0, 0),
        (R_HEAD, 0),
        (R_HEAD, HEAD_MARGIN),
        (CONE_TOP_R, Z_CONE_TOP),
        (0, Z_CONE_TOP),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
)

# ---------------- helical thread: tooth swept along a helix, fused to a core ----------------
half = math.radians(FLANK_ANGLE / 2.0)
tan_h, sin_h, cos_h = math.tan(half), math.sin(half), math.cos(half)
half_crest = CREST_FLAT / 2.0
gap_half = PITCH / 2.0 - half_crest            # half width of the thread space at the major diameter
r_vertex = R_MAJ - gap_half / tan_h            # apex of the (sharp) V between two teeth
rho = (R_MIN - r_vertex) / (1.0 / sin_h - 1.0) # root radius: rounded root bottoms out on D_MINOR
r_c = r_vertex + rho / sin_h                   # radius of the root-arc centres (at z = +-P/2)
r_tan = r_c - rho * sin_h                      # where the root arc meets the straight flank
z_tan = PITCH / 2.0 - rho * cos_h

CORE_LIFT = 0.02                               # core sits just above the arc bottom (clean boolean)
ARC_END = 0.01                                 # tooth foot leaves the arc just inside the core
phi_end = math.acos(1.0 - ARC_END / rho)
r_end = R_MIN + ARC_END
z_end_arc = PITCH / 2.0 - rho * math.sin(phi_end)
phi_mid = 0.5 * (phi_end + (math.pi / 2.0 - half))
r_mid = r_c - rho * math.cos(phi_mid)
z_mid = PITCH / 2.0 - rho * math.sin(phi_mid)
r_in = R_MIN - 0.15                            # foot of the tooth buried in the core
z_in = z_end_arc - 0.10

tooth = (
    cq.Workplane("XZ")
    .moveTo(r_in, -z_in)
    .lineTo(r_end, -z_end_arc)
    .threePointArc((r_mid, -z_mid), (r_tan, -z_tan))
    .lineTo(R_MAJ, -half_crest)
    .lineTo(R_MAJ, half_crest)
    .lineTo(r_tan, z_tan)
    .threePointArc((r_mid, z_mid), (r_end, z_end_arc))
    .lineTo(r_in, z_in)
    .close()
)

# start well inside the head, phased so a crest sits THREAD_PHASE*P below the end on +X
z_first = Z_TOP - THREAD_PHASE * PITCH
n_below = math.ceil((z_first - (Z_CONE_TOP - 1.5 * PITCH)) / PITCH)
z0 = z_first - n_below * PITCH
thread_len = (Z_TOP + 1.5 * PITCH) - z0

helix = cq.Wire.makeHelix(PITCH, thread_len, r_in)
thread = tooth.sweep(cq.Workplane("XY").add(helix), isFrenet=True).translate((0, 0, z0))

core = (
    cq.Workplane("XY")
    .workplane(offset=z0)
    .circle(R_MIN + CORE_LIFT)
    .extrude(thread_len)
)
shank = core.union(thread)

# flat end of the screw
keep = (
    cq.Workplane("XY")
    .workplane(offset=z0 - 1.0)
    .circle(R_HEAD + 1.0)
    .extrude(Z_TOP - z0 + 1.0)
)
shank = shank.intersect(keep)

result = head.union(shank)
if len(result.solids().vals()) != 1:          # safety net for a fragile boolean
    result = head.union(shank, tol=1e-4)

VIEW = {"azimuth": 45, "elevation": 26}
